import cadquery as cq
from OCP.ShapeUpgrade import ShapeUpgrade_UnifySameDomain
from OCP.GeomConvert import GeomConvert_ApproxCurve
from OCP.GeomAbs import GeomAbs_C2
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge

# ---------------------------------------------------------------------------
# Race-track desk model (Imola / "EMILIA ROMAGNA - ITALY"):
#   * a closed track outline strip standing on the base plane
#   * a name plate in front of it with a raised back lip, embossed F1 logo
#     and "ITALY"
#   * thick "EMILIA ROMAGNA" letters standing between plate and track
# ---------------------------------------------------------------------------

# ---- driving dimensions (mm) ----
TRACK_W = 4.2          # width of the track strip
TRACK_H = 3.5          # height of the track strip
TRACK_FILLET = 1.6     # rounding of the strip's top edges
TRACK_CORNER_R = 2.3   # centre-line radius at the sharp corners

PLATE_X0, PLATE_X1 = -100.0, 95.8    # plate length range
PLATE_Y0, PLATE_Y1 = -61.8, -44.1    # plate depth range
PLATE_T = 2.6                        # plate thickness
PLATE_END_R = 16.0                   # big rounding of the back-right corner
PLATE_CORNER_R = 1.5                 # small rounding of the back-left corner
LIP_W = 1.8                          # raised bead along the back edge
LIP_H = 0.8
LIP_X1 = 83.0
EMBOSS_H = 0.9                       # height of the F1 logo / ITALY

NAME_TEXT = "EMILIA ROMAGNA"
NAME_X0, NAME_X1 = -91.4, 41.3       # extent of the name letters
NAME_Y0, NAME_Y1 = -44.4, -38.7
NAME_H = 3.5

ITALY_X0, ITALY_X1 = 50.5, 80.2
ITALY_Y0, ITALY_Y1 = -55.0, -48.9

LOGO_X0, LOGO_Y0 = -91.9, -55.5      # F1 logo bounding box
LOGO_W, LOGO_HT = 22.8, 6.6

# transverse sector-marker grooves across the track: (x, y, track direction deg)
MARKERS = [(-88.0, -24.6, 43.6), (8.5, 10.4, 0.0), (48.8, 48.1, 0.0)]
MARKER_W, MARKER_D = 0.9, 0.8

# Track centre line: "c" = sharp corner, "s" = point on a smooth spline run
TRACK_NODES = [
    ("c", -100.7, -36.3),
    ("c", -76.0, -13.2),
    ("c", -77.6, -5.2),
    ("c", -59.7, 38.0),
    ("c", -46.8, 44.0),
    ("c", -45.8, 49.8),
    ("s", -36.9, 52.9),
    ("s", -29.5, 53.8),
    ("s", -19.7, 54.3),
    ("s", -10.0, 54.6),
    ("s", 0.0, 53.6),
    ("s", 8.7, 51.9),
    ("s", 17.4, 49.9),
    ("s", 23.9, 49.0),
    ("s", 33.7, 48.3),
    ("s", 42.9, 48.0),
    ("s", 49.4, 48.0),
    ("s", 55.9, 48.2),
    ("s", 61.1, 49.3),
    ("c", 67.1, 51.2),
    ("c", 91.9, 59.9),
    ("c", 98.5, 46.7),
    ("c", 85.6, 40.8),
    ("s", 79.7, 37.7),
    ("s", 73.9, 33.4),
    ("s", 67.8, 28.2),
    ("s", 61.7, 21.9),
    ("s", 50.8, 14.9),
    ("s", 43.0, 11.9),
    ("s", 37.1, 9.5),
    ("c", 31.9, 6.8),
    ("c", 29.5, 10.2),
    ("c", -16.0, 10.6),
    ("c", -22.9, 13.2),
    ("c", -30.5, 3.2),
    ("s", -29.4, -2.8),
    ("s", -27.5, -10.5),
    ("s", -26.3, -17.7),
    ("s", -27.2, -23.4),
    ("s", -29.3, -28.4),
    ("s", -31.6, -33.2),
    ("c", -33.2, -36.4),
    ("s", -38.8, -36.5),
    ("s", -45.6, -35.7),
    ("s", -52.3, -34.8),
    ("s", -59.1, -34.3),
    ("s", -67.5, -34.8),
    ("s", -76.3, -35.9),
    ("s", -86.1, -36.7),
    ("s", -93.7, -37.1),

]


def centre_line(nodes):
    """Closed wire of straight lines / splines, split at the sharp corners."""
    n = len(nodes)
    start = next(i for i, nd in enumerate(nodes) if nd[0] == "c")
    seq = nodes[start:] + nodes[:start] + [nodes[start]]
    edges, run = [], [seq[0]]
    for nd in seq[1:]:
        run.append(nd)
        if nd[0] == "c":
            pts = [cq.Vector(p[1], p[2], 0) for p in run]
            if len(pts) == 2:
                edges.append(cq.Edge.makeLine(pts[0], pts[1]))
            else:
                edges.append(cq.Edge.makeSpline(pts))
            run = [nd]
    return cq.Wire.assembleEdges(edges)


def unify(shape):
    """Merge the tangent-continuous pieces of the offset outlines into single edges."""
    u = ShapeUpgrade_UnifySameDomain(shape.wrapped, True, True, True)
    u.SetAngularTolerance(0.01)
    u.Build()
    return cq.Shape.cast(u.Shape())


def light_wire(wire, tol=0.005):
    """Re-approximate each (high-degree) edge by a compact C2 B-spline."""
    edges = []
    for e in wire.Edges():
        approx = GeomConvert_ApproxCurve(e._geomAdaptor().BSpline(), tol, GeomAbs_C2, 200, 5)
        edges.append(cq.Edge(BRepBuilderAPI_MakeEdge(approx.Curve()).Edge()))
    return cq.Wire.assembleEdges(edges)


def track_strip():
    w = centre_line(TRACK_NODES).fillet(TRACK_CORNER_R)
    outer = w.offset2D(TRACK_W / 2, "arc")[0]
    inner = w.offset2D(-TRACK_W / 2, "arc")[0]
    face = unify(cq.Face.makeFromWires(outer, [inner]).toNURBS())
    face = face if isinstance(face, cq.Face) else face.Faces()[0]
    face = cq.Face.makeFromWires(
        light_wire(face.outerWire()), [light_wire(w) for w in face.innerWires()]
    )
    solid = cq.Solid.extrudeLinear(face, cq.Vector(0, 0, TRACK_H))
    strip = cq.Workplane("XY").add(solid).faces(">Z").edges().fillet(TRACK_FILLET)
    cutters = []
    for (mx, my, ang) in MARKERS:
        cutters.append(
            cq.Workplane("XY", origin=(mx, my, TRACK_H - MARKER_D))
            .transformed(rotate=(0, 0, ang))
            .rect(MARKER_W, TRACK_W * 2)
            .extrude(MARKER_D + 1.0)
            .val()
        )
    return strip.cut(cq.Compound.makeCompound(cutters))


def plate():
    L = PLATE_X1 - PLATE_X0
    D = PLATE_Y1 - PLATE_Y0
    p = (
        cq.Workplane("XY")
        .center(PLATE_X0 + L / 2, PLATE_Y0 + D / 2)
        .rect(L, D)
        .extrude(PLATE_T)
    )
    p = p.edges("|Z and >X and >Y").fillet(PLATE_END_R)
    p = p.edges("|Z and <X and >Y").fillet(PLATE_CORNER_R)
    # raised lip along the back edge
    lip = (
        cq.Workplane("XY", origin=(0, 0, PLATE_T))
        .center((PLATE_X0 + LIP_X1) / 2, PLATE_Y1 - LIP_W / 2)
        .rect(LIP_X1 - PLATE_X0, LIP_W)
        .extrude(LIP_H)
        .edges("|X and >Z")
        .fillet(LIP_H * 0.95)
    )
    return p.union(lip)


def stretched_text(txt, x0, x1, y0, y1, height, bold=False):
    kind = "bold" if bold else "regular"
    t = cq.Workplane("XY").text(txt, 10.0, height, kind=kind, halign="left", valign="bottom")
    s = t.val() if len(t.vals()) == 1 else cq.Compound.makeCompound(t.vals())
    bb = s.BoundingBox()
    sx = (x1 - x0) / (bb.xmax - bb.xmin)
    sy = (y1 - y0) / (bb.ymax - bb.ymin)
    m = cq.Matrix([[sx, 0, 0, x0 - bb.xmin * sx],
                   [0, sy, 0, y0 - bb.ymin * sy],
                   [0, 0, 1, 0]])
    return s.transformGeometry(m)


def f1_logo(z0):
    x0, y0, w, h = LOGO_X0, LOGO_Y0, LOGO_W, LOGO_HT

    def P(u, v):
        return (x0 + u * w, y0 + v * h)

    # "F": slanted stem sweeping round into the top bar
    f_top = [P(0.0, 0.0), P(0.17, 0.0), P(0.355, 0.727), P(0.742, 0.727), P(0.815, 1.0),
             P(0.29, 1.0), P(0.234, 0.955)]
    # middle bar of the F (a separate stroke)
    f_mid = [P(0.274, 0.30), P(0.645, 0.30), P(0.694, 0.53), P(0.331, 0.53)]
    # the "1"
    one = [P(0.597, 0.0), P(0.726, 0.0), P(1.0, 1.0), P(0.887, 1.0)]
    wp = cq.Workplane("XY", origin=(0, 0, z0))
    out = None
    for poly in (f_top, f_mid, one):
        s = wp.polyline(poly).close().extrude(EMBOSS_H)
        out = s if out is None else out.union(s)
    return out


track = track_strip()
base = plate()
name = stretched_text(NAME_TEXT, NAME_X0, NAME_X1, NAME_Y0, NAME_Y1, NAME_H, bold=True)
italy = stretched_text("ITALY", ITALY_X0, ITALY_X1, ITALY_Y0, ITALY_Y1, PLATE_T + EMBOSS_H, bold=True)
logo = f1_logo(PLATE_T)

stand = (
    base.union(logo)
    .union(cq.Workplane("XY").add(italy))
    .union(cq.Workplane("XY").add(name))
)

# the track touches the stand only along the letter tops, so the two are kept
# as separate bodies of one compound
result = cq.Workplane("XY").add(
    cq.Compound.makeCompound(stand.solids().vals() + track.solids().vals())
)
